import cadquery as cq

# Axisymmetric roller / wheel: plain cylindrical tyre with an annular
# recess on both faces, a central hub flush with the faces and a through bore.

# ---------------- driving dimensions (mm) ----------------
OD = 50.0              # outer diameter of the roller
H = 32.6               # overall height (axial length)
RECESS_D = 37.8        # outer diameter of the annular recess on each face
HUB_D = 20.2           # hub outer diameter
HOLE_D = 11.2          # through bore
RECESS_DEPTH = 7.5     # depth of the annular recess (each face)
HUB_DROP = 0.0         # hub face below the rim face (0 = flush)

R_OUT_FILLET = 2.6     # outer rim edge round
R_RIM_IN_FILLET = 0.6  # recess mouth round
R_FLOOR_FILLET = 0.4   # recess floor corners (wall and hub side)
R_HUB_FILLET = 0.9     # hub outer face edge
R_HOLE_FILLET = 1.0    # bore entry edge
SEAM_ANGLE = 135.0     # rotate about the axis (only moves the revolve seam)

VIEW = {"azimuth": 45, "elevation": 26}

R = OD / 2
Rr = RECESS_D / 2
Rh = HUB_D / 2
Rb = HOLE_D / 2
zt = H / 2                 # rim face height
zf = zt - RECESS_DEPTH     # recess floor height
zh = zt - HUB_DROP         # hub face height

# half cross-section (r, z), symmetric about z = 0, revolved about the Z axis
profile = [
    (Rb, -zh), (Rh, -zh), (Rh, -zf), (Rr, -zf), (Rr, -zt), (R, -zt),
    (R, zt), (Rr, zt), (Rr, zf), (Rh, zf), (Rh, zh), (Rb, zh),
]
body = (
    cq.Workplane("XZ")
    .polyline(profile).close()
    .revolve(360, (0, 0, 0), (0, 1, 0))
)


def ring_edges(radius, zs, tol=0.05):
    """edge filter: circular edges of a given radius lying at one of the heights zs"""
    def pick(e):
        if e.geomType() != "CIRCLE" or abs(e.radius() - radius) > tol:
            return False
        return any(abs(e.Center().z - z) < tol for z in zs)
    return pick


def round_ring(wp, radius, zs, r):
    if r <= 0:
        return wp
    return wp.edges().filter(ring_edges(radius, zs)).fillet(r)


both = lambda z: [z, -z]
body = round_ring(body, R, both(zt), R_OUT_FILLET)       # outer rim edges
body = round_ring(body, Rr, both(zf), R_FLOOR_FILLET)    # recess floor / wall
body = round_ring(body, Rh, both(zf), R_FLOOR_FILLET)    # recess floor / hub
body = round_ring(body, Rr, both(zt), R_RIM_IN_FILLET)   # recess mouth
body = round_ring(body, Rh, both(zh), R_HUB_FILLET)      # hub face outer edge
body = round_ring(body, Rb, both(zh), R_HOLE_FILLET)     # bore entry

result = body.rotate((0, 0, 0), (0, 0, 1), SEAM_ANGLE)
